import cadquery as cq
import math

# ---------------- driving dimensions ----------------
# local frame: x along the lever (block at +x), z "up" in the lever plane, y = lever width direction.
TILT = -35.0          # rotation of the whole part about world X (deg)

ARM_Y0 = 17.0         # arm front face (y)
ARM_W = 18.5          # arm width (y)
ARM_R = 1.8           # arm long-edge fillet
ARM_R_V = 1.5         # arm profile-corner fillet
BLK_R_F = 3.5         # block / pad outline fillet, front face
BLK_R_B = 2.0         # block / pad outline fillet, back face

BLK_Y1 = 51.0         # block / pad depth in y (front face at y=0)
PAD_X0 = 172.5        # start of the full-depth pad (step)
PAD_ZT, PAD_ZB = -18.0, -33.4
BLK_X0, BLK_X1 = 214.5, 236.8   # block body x-range (BLK_X1 = +x face at z=0)
BLK_ZT = 1.6                     # block top
XFACE_TILT = 2.8                 # +x face leans inwards towards the ear ends (deg)
R_TL, R_TR = 8.0, 13.0           # block top rounds
R_PAD_TOP = 10.0                 # concave round pad top -> block
EAR_XL = 207.7                   # ear left edge
R_PAD_BOT = 22.0                 # concave round pad bottom -> ear left edge
EAR_ZB = -79.8                   # ear bottom
R_EAR_L, R_EAR_R = 9.0, 11.0     # ear bottom corner rounds
GAP_Z = -41.5                    # clevis gap ceiling
EAR_T1 = 8.0                     # front ear thickness
EAR_Y2, EAR_Y3 = 33.3, 41.0      # rear ear y-range
SLOT_W, SLOT_L = 12.0, 19.5      # slot in rear ear
SLOT_XC, SLOT_ZC = 221.2, -64.5

# ---------------- arm profile (x,z) ----------------
outer = [(-4.5, -15.4), (-1.0, -11.2), (5.4, -7.6), (9.9, -4.4), (12.3, -1.0), (13.9, 3.6),
         (18.1, 7.7), (28.0, 13.2), (40.1, 18.7), (53.1, 22.6), (65.3, 24.4), (76.0, 24.5),
         (86.0, 22.4), (96.7, 18.5), (109.7, 11.2), (120.8, 3.2), (130.1, -5.2), (137.8, -10.9),
         (148.3, -14.4), (160.7, -16.8), (PAD_X0 + 3.0, PAD_ZT)]
inner = [(PAD_X0 + 3.0, PAD_ZB), (162.5, -32.0), (149.5, -31.3), (139.4, -29.1), (128.1, -24.5),
         (117.7, -17.9), (109.2, -10.6), (98.1, -2.6), (85.9, 3.4), (75.4, 6.5), (62.4, 6.4),
         (46.8, 3.2), (37.5, 0.4), (31.5, -2.6)]
hook_in = [(31.5, -2.6), (28.4, -6.4), (26.3, -12.0), (25.6, -18.5), (25.3, -21.6)]

def arm_solid():
    wp = cq.Workplane("XZ")
    prof = (wp.moveTo(*outer[0]).spline(outer[1:], includeCurrent=True)
            .lineTo(*inner[0]).spline(inner[1:], includeCurrent=True)
            .spline(hook_in[1:], includeCurrent=True)
            .threePointArc((24.7, -23.2), (23.3, -23.7))   # rounded inner-bottom corner
            .lineTo(20.5, -23.7)                           # hook bottom
            .threePointArc((17.9, -21.6), (15.5, -19.2))   # concave sweep up to the lip
            .lineTo(-2.2, -19.0)                           # lip underside
            .threePointArc((-4.0, -18.4), (-4.5, -17.0))   # rounded nose
            .close())
    s = prof.extrude(-ARM_W).translate((0, ARM_Y0, 0))
    s = s.edges("|Y").fillet(ARM_R_V)
    s = s.faces("<Y or >Y").edges().fillet(ARM_R)
    return s

arm = arm_solid()

# ---------------- block + pad + ears profile, extruded over full depth ----------------
def pt(c, r, a):
    return (c[0] + r * math.cos(math.radians(a)), c[1] + r * math.sin(math.radians(a)))

def block_solid():
    a = math.radians(XFACE_TILT)                           # +x face leans in towards the bottom
    n = (math.cos(a), -math.sin(a))                         # outward normal of the +x face
    x_at = lambda z: BLK_X1 + math.tan(a) * z               # +x face: x as a function of z
    c1 = (BLK_X0 - R_PAD_TOP, PAD_ZT + R_PAD_TOP)          # concave pad-top round
    c2 = (BLK_X0 + R_TL, BLK_ZT - R_TL)                    # top-left convex round
    c3 = (BLK_X1 + (math.sin(a) * (BLK_ZT - R_TR) - R_TR) / math.cos(a), BLK_ZT - R_TR)   # top-right round
    c5 = (BLK_X1 + (math.sin(a) * (EAR_ZB + R_EAR_R) - R_EAR_R) / math.cos(a), EAR_ZB + R_EAR_R)  # ear bottom-right
    c6 = (EAR_XL + R_EAR_L, EAR_ZB + R_EAR_L)              # ear bottom-left round
    c4 = (EAR_XL - R_PAD_BOT, PAD_ZB - R_PAD_BOT)          # concave pad-bottom round
    ang_n = -XFACE_TILT
    p = (cq.Workplane("XZ").moveTo(PAD_X0, PAD_ZT)
         .lineTo(*pt(c1, R_PAD_TOP, -90))
         .threePointArc(pt(c1, R_PAD_TOP, -45), pt(c1, R_PAD_TOP, 0))
         .lineTo(*pt(c2, R_TL, 180))
         .threePointArc(pt(c2, R_TL, 135), pt(c2, R_TL, 90))
         .lineTo(*pt(c3, R_TR, 90))
         .threePointArc(pt(c3, R_TR, (90 + ang_n) / 2), pt(c3, R_TR, ang_n))
         .lineTo(*pt(c5, R_EAR_R, ang_n))
         .threePointArc(pt(c5, R_EAR_R, (ang_n - 90) / 2), pt(c5, R_EAR_R, -90))
         .lineTo(*pt(c6, R_EAR_L, -90))
         .threePointArc(pt(c6, R_EAR_L, -135), pt(c6, R_EAR_L, 180))
         .lineTo(*pt(c4, R_PAD_BOT, 0))
         .threePointArc(pt(c4, R_PAD_BOT, 45), pt(c4, R_PAD_BOT, 90))
         .lineTo(PAD_X0, PAD_ZB)
         .close())
    s = p.extrude(-BLK_Y1)
    s = s.faces("<Y").edges().fillet(BLK_R_F)   # front face (y=0)
    s = s.faces(">Y").edges().fillet(BLK_R_B)   # back face (y=BLK_Y1)
    # clevis gap and rear notch
    gap = cq.Workplane("XY").box(80, EAR_Y2 - EAR_T1, 60, centered=False).translate((180, EAR_T1, GAP_Z - 60))
    notch = cq.Workplane("XY").box(80, BLK_Y1 - EAR_Y3 + 5, 60, centered=False).translate((180, EAR_Y3, GAP_Z - 60))
    s = s.cut(gap).cut(notch)
    # slot through the rear ear
    slot = (cq.Workplane("XZ").center(SLOT_XC, SLOT_ZC).slot2D(SLOT_L, SLOT_W, angle=90)
            .extrude(-(EAR_Y3 - EAR_Y2) - 2).translate((0, EAR_Y2 - 1, 0)))
    s = s.cut(slot)
    return s

block = block_solid()
local = arm.union(block)

# blend the arm into the step face of the pad (concave junction edges)
JUNCTION_R = 5.0
def _junction_edges(shape):
    out = []
    for e in shape.Edges():
        bb = e.BoundingBox()
        on_step = abs(bb.xmin - PAD_X0) < 0.6 and abs(bb.xmax - PAD_X0) < 0.6
        in_arm = bb.ymin > ARM_Y0 - 0.5 and bb.ymax < ARM_Y0 + ARM_W + 0.5
        flush_top = abs(bb.zmin - PAD_ZT) < 0.01 and abs(bb.zmax - PAD_ZT) < 0.01
        if on_step and in_arm and not flush_top:
            out.append(e)
    return out
try:
    local = cq.Workplane("XY").add(local.val().fillet(JUNCTION_R, _junction_edges(local.val())))
except Exception:
    pass

result = local.rotate((0, 0, 0), (1, 0, 0), TILT)
